"""Dactyl-Manuform style split-keyboard case, left half.

4 rows x 5 columns of key plates on a curved, tented key well (bottom row only on
the middle and ring columns), two tall (1.5u) thumb keys, thin walls dropping to an
open bottom, five screw-insert bosses, a USB holder frame and a small slot in the
back wall.  The geometry follows the Dactyl-Manuform construction: every key is a
plate placed by a chain of translations / rotations, neighbouring plates are joined
by convex hulls of their corner posts, and the walls are hulls of the edge posts
and their projections onto the floor.
"""
import math
import itertools
import numpy as np
import cadquery as cq

# ----------------------------------------------------------- parameters ---
NROWS = 4
NCOLS = 5
ALPHA = math.pi / 12                  # curvature of the columns (per row)
BETA = math.pi / 36                   # curvature of the rows (per column)
CENTERROW = NROWS - 3
CENTERCOL = 4
TENTING = math.radians(26.0)          # tenting of the whole key well
KEYBOARD_Z_OFFSET = 9.0               # overall height
EXTRA_WIDTH = 2.5                     # extra space between key columns
EXTRA_HEIGHT = 1.0                    # extra space between key rows

WALL_Z_OFFSET = -15.0                 # drop of the first sloping part of a wall
WALL_XY_OFFSET = 5.0                  # outward offset of that sloping part
WALL_THICKNESS = 2.0
LEFT_WALL_X_OFFSET = 10.0             # inner (tented-up) wall stand-off
LEFT_WALL_Z_OFFSET = 3.0
THUMB_WALL_XY = 12.0                  # outward offset of the thumb walls
THUMB_SIDE_DY = -0.45                 # forward lean of the thumb side wall

THUMB_OFFSETS = (6.5, -1.5, 7.0)
THUMB_ROT = (10.0, -23.0, 10.0)       # thumb key rotations about x, y, z (deg)
THUMB_TR_SHIFT = (-12.0, -16.0, 3.0)
THUMB_TL_SHIFT = (-32.0, -15.0, -2.0)

KEYSWITCH = 14.4                      # square switch cut-out
PLATE_T = 4.0                         # key plate thickness
MOUNT = KEYSWITCH + 3.0               # key plate size
SA_HEIGHT = 12.7
CAP_TOP = PLATE_T + SA_HEIGHT
WEB_T = 3.5                           # thickness of the connecting web
SA_DOUBLE = 37.5                      # 2u key length, sets the 1.5u plate extension

COLUMN_OFFSETS = {2: (0.0, 2.82, -4.5), 4: (0.0, -12.0, 5.64)}   # middle / pinky stagger

# screw inserts (outer boss = insert + 1.6 mm wall)
INS_H = 3.8
INS_RB = 5.31 / 2
INS_RT = 5.1 / 2
INS_WALL = 1.6
INS_EXTRA_H = 1.5

# USB holder frame on the back wall next to the inner corner, and a small slot
USB_X = 73.8
USB_W = 14.6
USB_H = 22.4
USB_Y_BACK = 45.2
USB_DEPTH = 10.0
USB_HOLE_W = 10.3
USB_HOLE_H = 18.2
USB_HOLE_Z = 2.2
SLOT_X = 57.5
SLOT_W = 6.3
SLOT_H = 14.3
SLOT_Z = 1.5

MIRROR = True                          # build the left-hand half

# derived
LASTROW = NROWS - 1
CORNERROW = NROWS - 2
LASTCOL = NCOLS - 1
ROW_RADIUS = ((MOUNT + EXTRA_HEIGHT) / 2) / math.sin(ALPHA / 2) + CAP_TOP
COL_RADIUS = ((MOUNT + EXTRA_WIDTH) / 2) / math.sin(BETA / 2) + CAP_TOP


# ----------------------------------------------------------- placements ---
# A placement is a list of elementary operations applied in order:
#   ("T", (x, y, z))  translation,   ("R", axis, angle_rad)  rotation about x/y/z.
def op_matrix(op):
    m = np.eye(4)
    if op[0] == "T":
        m[:3, 3] = op[1]
        return m
    axis, a = op[1], op[2]
    c, s = math.cos(a), math.sin(a)
    i, j = {0: (1, 2), 1: (2, 0), 2: (0, 1)}[axis]
    m[i, i], m[i, j], m[j, i], m[j, j] = c, -s, s, c
    return m


def ops_matrix(ops):
    out = np.eye(4)
    for op in ops:
        out = op_matrix(op) @ out
    return out


def ops_location(ops):
    """cq.Location of the placement in the final (mirrored) frame.
    Mirroring x conjugates the chain: translations get -x, y/z rotations flip sign."""
    loc = cq.Location()
    for op in ops:
        if op[0] == "T":
            x, y, z = op[1]
            step = cq.Location(cq.Vector(-x if MIRROR else x, y, z))
        else:
            axis, a = op[1], op[2]
            if MIRROR and axis != 0:
                a = -a
            vec = cq.Vector(*[1.0 if k == axis else 0.0 for k in range(3)])
            step = cq.Location(cq.Vector(0, 0, 0), vec, math.degrees(a))
        loc = step * loc
    return loc


def key_ops(col, row):
    return [("T", (0, 0, -ROW_RADIUS)), ("R", 0, ALPHA * (CENTERROW - row)), ("T", (0, 0, ROW_RADIUS)),
            ("T", (0, 0, -COL_RADIUS)), ("R", 1, BETA * (CENTERCOL - col)), ("T", (0, 0, COL_RADIUS)),
            ("T", COLUMN_OFFSETS.get(col, (0.0, 0.0, 0.0))),
            ("R", 1, TENTING), ("T", (0, 0, KEYBOARD_Z_OFFSET))]


def apply(m, p):
    return m[:3, :3] @ np.asarray(p, dtype=float) + m[:3, 3]


def key_position(col, row, p):
    return apply(ops_matrix(key_ops(col, row)), p)


THUMB_ORIGIN = tuple(key_position(1, CORNERROW, [MOUNT / 2, -MOUNT / 2, 0]) + np.array(THUMB_OFFSETS))


def thumb_ops(shift):
    rx, ry, rz = (math.radians(a) for a in THUMB_ROT)
    return [("R", 0, rx), ("R", 1, ry), ("R", 2, rz), ("T", THUMB_ORIGIN), ("T", shift)]


def wpt(p):
    """unmirrored construction point -> final frame"""
    p = np.asarray(p, dtype=float)
    return p * np.array([-1.0, 1.0, 1.0]) if MIRROR else p


# ---------------------------------------------------------------- posts ---
# a post is a short vertical segment (two points) standing under a plate corner
H = MOUNT / 2
TH = MOUNT / 1.15                       # 1.5u thumb plate corner
P_TL, P_TR, P_BL, P_BR = (-H, H), (H, H), (-H, -H), (H, -H)
TP_TL, TP_TR, TP_BL, TP_BR = (-H, TH), (H, TH), (-H, -TH), (H, -TH)
P_C = (0.0, 0.0)


def post_local(x, y):
    return [np.array([x, y, PLATE_T - WEB_T]), np.array([x, y, PLATE_T])]


class Place:
    def __init__(self, ops):
        self.ops = ops
        self.m = ops_matrix(ops)

    def post(self, corner, off=(0.0, 0.0, 0.0)):
        """corner post, optionally offset in the local frame (like translate-before-place)"""
        return [wpt(apply(self.m, q + np.asarray(off, dtype=float))) for q in post_local(*corner)]


def KP(col, row):
    return Place(key_ops(col, row))


def LKP(row, direction):
    pos = key_position(0, row, [-MOUNT / 2, direction * MOUNT / 2, 0]) - np.array(
        [LEFT_WALL_X_OFFSET, 0, LEFT_WALL_Z_OFFSET])
    return Place([("T", tuple(pos))])


TR = Place(thumb_ops(THUMB_TR_SHIFT))
TL = Place(thumb_ops(THUMB_TL_SHIFT))


# ----------------------------------------------------------------- hull ---
def _hull2d(pts2):
    pts = sorted(set((round(p[0], 9), round(p[1], 9), i) for i, p in enumerate(pts2)))
    if len(pts) < 3:
        return [p[2] for p in pts]

    def cross(o, a, b):
        return (a[0] - o[0]) * (b[1] - o[1]) - (a[1] - o[1]) * (b[0] - o[0])
    lower, upper = [], []
    for p in pts:
        while len(lower) >= 2 and cross(lower[-2], lower[-1], p) <= 1e-12:
            lower.pop()
        lower.append(p)
    for p in reversed(pts):
        while len(upper) >= 2 and cross(upper[-2], upper[-1], p) <= 1e-12:
            upper.pop()
        upper.append(p)
    return [p[2] for p in lower[:-1] + upper[:-1]]


def hull_solid(points, tol=1e-5):
    """convex hull of a handful of post end points as a planar-faced solid"""
    uniq = []
    for p in np.array(points, dtype=float):
        if not any(np.linalg.norm(p - q) < 1e-6 for q in uniq):
            uniq.append(p)
    P = np.array(uniq)
    n = len(P)
    if n < 4:
        return None
    planes = []
    for i, j, k in itertools.combinations(range(n), 3):
        nv = np.cross(P[j] - P[i], P[k] - P[i])
        ln = np.linalg.norm(nv)
        if ln < 1e-9:
            continue
        nv = nv / ln
        d = nv @ P[i]
        dist = P @ nv - d
        if np.all(dist <= tol):
            cand = (nv, d)
        elif np.all(dist >= -tol):
            cand = (-nv, -d)
        else:
            continue
        if not any(np.dot(cand[0], q[0]) > 1 - 1e-9 and abs(cand[1] - q[1]) < 1e-6 for q in planes):
            planes.append(cand)
    if len(planes) < 4:
        return None
    faces = []
    for nv, d in planes:
        idx = [i for i in range(n) if abs(P[i] @ nv - d) <= tol]
        a = np.array([1.0, 0, 0]) if abs(nv[0]) < 0.9 else np.array([0, 1.0, 0])
        u = np.cross(nv, a)
        u /= np.linalg.norm(u)
        v = np.cross(nv, u)
        order = _hull2d([(P[i] @ u, P[i] @ v) for i in idx])
        if len(order) < 3:
            continue
        wire = cq.Wire.makePolygon([cq.Vector(*P[idx[o]]) for o in order], close=True)
        faces.append(cq.Face.makeFromWires(wire))
    sol = cq.Solid.makeSolid(cq.Shell.makeShell(faces))
    if sol.Volume() < 0:
        sol = cq.Solid(sol.wrapped.Reversed())
    return sol


def hull(*posts):
    return hull_solid([p for post in posts for p in post])


def triangle_hulls(*posts):
    out = []
    for i in range(len(posts) - 2):
        s = hull(posts[i], posts[i + 1], posts[i + 2])
        if s is not None:
            out.append(s)
    return out


# ---------------------------------------------------------------- walls ---
FLOOR_Z = -3.0                          # walls run below the floor and are cut flat at z = 0


def wl1(dx, dy):
    return (dx * WALL_THICKNESS, dy * WALL_THICKNESS, -1.0)


def wl2(dx, dy, xy=WALL_XY_OFFSET):
    return (dx * xy, dy * xy, WALL_Z_OFFSET)


def wl3(dx, dy, xy=WALL_XY_OFFSET):
    return (dx * (xy + WALL_THICKNESS), dy * (xy + WALL_THICKNESS), WALL_Z_OFFSET)


def floor_proj(post):
    return [np.array([post[0][0], post[0][1], FLOOR_Z])]


def side_points(pl, dx, dy, c, xy):
    """upper and lower post sets of one end of a wall brace; xy=None -> plain vertical drop"""
    if xy is None:
        p = pl.post(c)
        return [p], [p]
    a2, a3 = pl.post(c, wl2(dx, dy, xy)), pl.post(c, wl3(dx, dy, xy))
    return [pl.post(c), pl.post(c, wl1(dx, dy)), a2, a3], [a2, a3]


def wall_brace(pl1, dx1, dy1, c1, pl2, dx2, dy2, c2, xy1=WALL_XY_OFFSET, xy2=WALL_XY_OFFSET):
    up1, lo1 = side_points(pl1, dx1, dy1, c1, xy1)
    up2, lo2 = side_points(pl2, dx2, dy2, c2, xy2)
    out = []
    s = hull(*(up1 + up2))
    if s is not None:
        out.append(s)
    low = lo1 + lo2
    s = hull(*(low + [floor_proj(p) for p in low]))
    if s is not None:
        out.append(s)
    return out


def key_wall_brace(x1, y1, dx1, dy1, c1, x2, y2, dx2, dy2, c2):
    return wall_brace(KP(x1, y1), dx1, dy1, c1, KP(x2, y2), dx2, dy2, c2)


# --------------------------------------------------------------- plates ---
def plate_local():
    outer = cq.Solid.makeBox(MOUNT, MOUNT, PLATE_T, cq.Vector(-MOUNT / 2, -MOUNT / 2, 0))
    hole = cq.Solid.makeBox(KEYSWITCH, KEYSWITCH, PLATE_T + 2, cq.Vector(-KEYSWITCH / 2, -KEYSWITCH / 2, -1))
    return outer.cut(hole)


def larger_plate_local():
    ph = (SA_DOUBLE - MOUNT) / 3
    a = cq.Solid.makeBox(MOUNT, ph, WEB_T, cq.Vector(-MOUNT / 2, MOUNT / 2, PLATE_T - WEB_T))
    b = cq.Solid.makeBox(MOUNT, ph, WEB_T, cq.Vector(-MOUNT / 2, -MOUNT / 2 - ph, PLATE_T - WEB_T))
    return a.fuse(b)


def has_key(col, row):
    return col in (2, 3) or row != LASTROW


def build():
    parts = []
    plate = plate_local()
    big = larger_plate_local()

    # key plates
    for col in range(NCOLS):
        for row in range(NROWS):
            if has_key(col, row):
                parts.append(plate.moved(ops_location(key_ops(col, row))))
    for pl in (TR, TL):
        loc = ops_location(pl.ops)
        parts.append(plate.moved(loc))
        parts.append(big.moved(loc))

    # web between neighbouring plates
    for col in range(NCOLS - 1):
        for row in range(LASTROW):
            parts += triangle_hulls(KP(col + 1, row).post(P_TL), KP(col, row).post(P_TR),
                                    KP(col + 1, row).post(P_BL), KP(col, row).post(P_BR))
    for col in range(NCOLS):
        for row in range(CORNERROW):
            parts += triangle_hulls(KP(col, row).post(P_BL), KP(col, row).post(P_BR),
                                    KP(col, row + 1).post(P_TL), KP(col, row + 1).post(P_TR))
    for col in range(NCOLS - 1):
        for row in range(CORNERROW):
            parts += triangle_hulls(KP(col, row).post(P_BR), KP(col, row + 1).post(P_TR),
                                    KP(col + 1, row).post(P_BL), KP(col + 1, row + 1).post(P_TL))
    parts += triangle_hulls(KP(2, LASTROW).post(P_TR), KP(2, LASTROW).post(P_BR),
                            KP(3, LASTROW).post(P_TL), KP(3, LASTROW).post(P_BL))
    for col in (2, 3):
        parts += triangle_hulls(KP(col, CORNERROW).post(P_BL), KP(col, CORNERROW).post(P_BR),
                                KP(col, LASTROW).post(P_TL), KP(col, LASTROW).post(P_TR))
    parts += triangle_hulls(KP(2, CORNERROW).post(P_BR), KP(2, LASTROW).post(P_TR),
                            KP(3, CORNERROW).post(P_BL), KP(3, LASTROW).post(P_TL))

    # thumb web
    parts += triangle_hulls(TL.post(TP_TR), TL.post(TP_BR), TR.post(TP_TL), TR.post(TP_BL))
    parts += triangle_hulls(
        TL.post(TP_TL), KP(0, CORNERROW).post(P_BL), TL.post(TP_TR), KP(0, CORNERROW).post(P_BR),
        TR.post(TP_TL), KP(1, CORNERROW).post(P_BL), TR.post(TP_TR), KP(1, CORNERROW).post(P_BR),
        KP(2, LASTROW).post(P_TL), KP(2, LASTROW).post(P_BL), TR.post(TP_TR),
        KP(2, LASTROW).post(P_BL), TR.post(TP_BR), KP(2, LASTROW).post(P_BR),
        KP(3, LASTROW).post(P_BL), KP(2, LASTROW).post(P_TR), KP(3, LASTROW).post(P_TL),
        KP(3, CORNERROW).post(P_BL), KP(3, LASTROW).post(P_TR), KP(3, CORNERROW).post(P_BR),
        KP(4, CORNERROW).post(P_BL))
    parts += triangle_hulls(KP(1, CORNERROW).post(P_BR), KP(2, LASTROW).post(P_TL),
                            KP(2, CORNERROW).post(P_BL), KP(2, LASTROW).post(P_TR),
                            KP(2, CORNERROW).post(P_BR), KP(3, CORNERROW).post(P_BL))
    parts += triangle_hulls(KP(3, LASTROW).post(P_TR), KP(3, LASTROW).post(P_BR),
                            KP(4, CORNERROW).post(P_BL))

    # case walls
    walls = []
    # back wall
    for x in range(NCOLS):
        walls += key_wall_brace(x, 0, 0, 1, P_TL, x, 0, 0, 1, P_TR)
    for x in range(1, NCOLS):
        walls += key_wall_brace(x, 0, 0, 1, P_TL, x - 1, 0, 0, 1, P_TR)
    walls += key_wall_brace(LASTCOL, 0, 0, 1, P_TR, LASTCOL, 0, 1, 0, P_TR)
    # outer (pinky) wall
    for y in range(LASTROW):
        walls += key_wall_brace(LASTCOL, y, 1, 0, P_TR, LASTCOL, y, 1, 0, P_BR)
    for y in range(1, LASTROW):
        walls += key_wall_brace(LASTCOL, y - 1, 1, 0, P_BR, LASTCOL, y, 1, 0, P_TR)
    walls += key_wall_brace(LASTCOL, CORNERROW, 0, -1, P_BR, LASTCOL, CORNERROW, 1, 0, P_BR)
    # inner (tented-up) wall
    for y in range(LASTROW):
        walls += wall_brace(LKP(y, 1), -1, 0, P_C, LKP(y, -1), -1, 0, P_C)
        walls.append(hull(KP(0, y).post(P_TL), KP(0, y).post(P_BL), LKP(y, 1).post(P_C), LKP(y, -1).post(P_C)))
    for y in range(1, LASTROW):
        walls += wall_brace(LKP(y - 1, -1), -1, 0, P_C, LKP(y, 1), -1, 0, P_C)
        walls.append(hull(KP(0, y).post(P_TL), KP(0, y - 1).post(P_BL),
                          LKP(y, 1).post(P_C), LKP(y - 1, -1).post(P_C)))
    walls += wall_brace(KP(0, 0), 0, 1, P_TL, LKP(0, 1), 0, 1, P_C)
    walls += wall_brace(LKP(0, 1), 0, 1, P_C, LKP(0, 1), -1, 0, P_C)
    # front wall
    walls += key_wall_brace(3, LASTROW, 0, -1, P_BL, 3, LASTROW, 0.5, -1, P_BR)
    walls += key_wall_brace(3, LASTROW, 0.5, -1, P_BR, 4, CORNERROW, 1, -1, P_BL)
    walls += key_wall_brace(4, CORNERROW, 0, -1, P_BL, 4, CORNERROW, 0, -1, P_BR)
    # thumb walls
    q, sdy = THUMB_WALL_XY, THUMB_SIDE_DY
    walls += wall_brace(TR, 0, -1, TP_BR, KP(3, LASTROW), 0, -1, P_BL, None, WALL_XY_OFFSET)
    walls += wall_brace(TR, 0, -1, TP_BR, TR, 0, -1, TP_BL, None, q)
    walls += wall_brace(TR, 0, -1, TP_BL, TL, 0, -1, TP_BR, q, q)
    walls += wall_brace(TL, 0, -1, TP_BR, TL, 0, -1, TP_BL, q, q)
    walls += wall_brace(TL, 0, -1, TP_BL, TL, -1, sdy, TP_BL, q, q)
    walls += wall_brace(TL, -1, sdy, TP_BL, TL, -1, sdy, TP_TL, q, q)
    walls += wall_brace(TL, -1, sdy, TP_TL, LKP(CORNERROW, -1), -1, 0, P_C, q, WALL_XY_OFFSET)
    walls.append(hull(TL.post(TP_TL), KP(0, CORNERROW).post(P_BL), LKP(CORNERROW, -1).post(P_C)))
    parts += [w for w in walls if w is not None]
    return parts


# --------------------------------------------------------- screw inserts ---
def screw_pos(col, row):
    shift_right = col == LASTCOL
    shift_left = col == 0
    shift_up = (not (shift_right or shift_left)) and row == 0
    shift_down = (not (shift_right or shift_left)) and row >= LASTROW
    if shift_up:
        p = key_position(col, row, np.array(wl2(0, 1)) + [0, MOUNT / 2, 0])
    elif shift_down:
        p = key_position(col, row, np.array(wl2(0, -1)) - [0, MOUNT / 2, 0])
    elif shift_left:
        p = (key_position(0, row, [-MOUNT / 2, 0, 0])
             - np.array([LEFT_WALL_X_OFFSET, 0, LEFT_WALL_Z_OFFSET]) + np.array(wl3(-1, 0)))
    else:
        p = key_position(col, row, np.array(wl2(1, 0)) + [MOUNT / 2, 0, 0])
    return wpt(p)


SCREWS = [(0, 0), (0, CORNERROW), (2, LASTROW + 0.3), (3, 0), (LASTCOL, 1)]


def insert_shape(rb, rt, h, pos):
    """tapered post with a domed top"""
    cyl = cq.Solid.makeCone(rb, rt, h, cq.Vector(pos[0], pos[1], 0))
    dome = cq.Solid.makeSphere(rt, cq.Vector(pos[0], pos[1], h), angleDegrees1=0, angleDegrees2=90)
    return cyl.fuse(dome)


def usb_parts():
    y0 = USB_Y_BACK - USB_DEPTH
    frame = cq.Solid.makeBox(USB_W, USB_DEPTH, USB_H, cq.Vector(USB_X - USB_W / 2, y0, 0))
    opening = cq.Solid.makeBox(USB_HOLE_W, USB_DEPTH + 20, USB_HOLE_H,
                               cq.Vector(USB_X - USB_HOLE_W / 2, y0 - 10, USB_HOLE_Z))
    slot = cq.Solid.makeBox(SLOT_W, 30, SLOT_H, cq.Vector(SLOT_X - SLOT_W / 2, USB_Y_BACK - 25, SLOT_Z))
    return frame, opening, slot


# ---------------------------------------------------------------- model ---
parts = build()
body = parts[0].fuse(*parts[1:])

boss_outer = [insert_shape(INS_RB + INS_WALL, INS_RT + INS_WALL, INS_H + INS_EXTRA_H, screw_pos(c, r))
              for c, r in SCREWS]
boss_hole = [insert_shape(INS_RB, INS_RT, INS_H, screw_pos(c, r)) for c, r in SCREWS]
usb_frame, usb_opening, back_slot = usb_parts()

body = body.fuse(*boss_outer, usb_frame)
body = body.cut(boss_hole[0].fuse(*boss_hole[1:], usb_opening, back_slot))
body = body.cut(cq.Solid.makeBox(400, 400, 50, cq.Vector(-200, -200, -50)))   # flat floor at z = 0
body = body.clean()

result = cq.Workplane("XY").add(body)

VIEW = {"azimuth": 45, "elevation": 26}
